import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 5.0            # strap thickness
W = 24.0           # strap width (Y)
EDGE_R = 1.2       # rounding of the long strap edges
R_LEG = 137.5      # half distance between leg centre lines (= outer band centre radius)
Z_TOP = 254.0      # top of the hooks
R_IN = 169.0       # centre-line radius of the inner (perforated) arc
Z_IN_BOT = 60.9    # centre-line height of the inner arc at its lowest point
R_BEND = 28.0      # inside radius where the inner arc leaves the leg
R_CROTCH = 3.0     # fillet radius in the crotch between inner arc and outer band

# hooks
HOOK_X = 148.0     # |x| of the outside of the hook lip
HOOK_T = 3.0       # hook material thickness
HOOK_DROP = 9.3    # lip length measured from the top
W_HOOK = 18.0      # hook width
NOTCH_H = 5.0      # height of the narrow part at the top of the legs

# holes
ARC_HOLE_L = 19.5  # oval holes of the inner arc (along strap / across strap)
ARC_HOLE_W = 11.5
LEG_HOLE_L = 17.0  # oval holes in the legs
LEG_HOLE_W = 10.0
LEG_HOLE_Z = [222.0, 190.0, 158.0]
ARC_HOLE_STEP = 9.7  # degrees between the holes of the inner arc
ARC_HOLE_N = 9

# latch tabs on the outer band
TAB_PHI = 60.5     # angular position (from bottom) of the tab root on the outer band
TAB_FLARE = 12.0   # flare angle of the tab away from the band
TAB_L = 24.0
TAB_T = 2.5
TAB_W = 22.0

# pegs (short cross pins, axis along Y, flush with the -Y edge of the band)
PEG_D = 5.6
PEG_LEN = 5.6
TAB_PEG_Z = 75.4
PEG_EMBED = 0.6     # overlap of the tab peg with the tab
BOT_PEG_X = 50.4
BOT_PEG_EMBED = 2.0  # how far the bottom pegs sink into the band

# perforation slits along the -Y edge of the outer band
SLIT_EDGE = 3.0    # distance of the slit centre from the -Y edge
SLIT_W = 0.9
SLIT_LEN = 19.0
SLIT_PITCH = 24.8
SLIT_N = 8         # per side (plus one in the middle)
SLIT_DEPTH = 1.2

# ---------------- derived values ----------------
ZC_O = R_LEG + T / 2.0                 # centre of the outer band
RO_OUT = R_LEG + T / 2.0               # outer band outside radius
RO_IN = R_LEG - T / 2.0                # outer band inside radius
ZC_I = Z_IN_BOT + R_IN                 # centre of the inner arc
RA_UP = R_IN - T / 2.0                 # inner arc concave (upper) surface
RA_LO = R_IN + T / 2.0                 # inner arc convex (lower) surface
X_LI = R_LEG - T / 2.0                 # leg inside face |x|
X_LO = R_LEG + T / 2.0                 # leg outside face |x|
Z_LEG_TOP = Z_TOP                      # legs run full width up to the top


def unit(vx, vz):
    n = math.hypot(vx, vz)
    return vx / n, vz / n


def arc_mid(c, r, p0, p1):
    """mid point of the (shorter) arc of circle (c,r) between p0 and p1"""
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    da = a1 - a0
    while da > math.pi:
        da -= 2 * math.pi
    while da < -math.pi:
        da += 2 * math.pi
    am = a0 + da / 2.0
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def mx(p):
    return (-p[0], p[1])


# --- bend fillet between leg inside face and inner arc (right side, x>0) ---
fx = X_LI - R_BEND
fz = ZC_I - math.sqrt((RA_UP - R_BEND) ** 2 - fx ** 2)
bend_on_leg = (X_LI, fz)
ux, uz = unit(fx, fz - ZC_I)
bend_on_arc = (RA_UP * ux, ZC_I + RA_UP * uz)
bend_mid = arc_mid((fx, fz), R_BEND, bend_on_leg, bend_on_arc)

# --- crotch fillet between inner arc lower face and outer band inside face ---
rA = RA_LO + R_CROTCH
rB = RO_IN - R_CROTCH
zc = (rA ** 2 - rB ** 2 - ZC_I ** 2 + ZC_O ** 2) / (2.0 * (ZC_O - ZC_I))
xc = math.sqrt(rB ** 2 - (zc - ZC_O) ** 2)
ux, uz = unit(xc, zc - ZC_I)
crotch_on_A = (RA_LO * ux, ZC_I + RA_LO * uz)
ux, uz = unit(xc, zc - ZC_O)
crotch_on_B = (RO_IN * ux, ZC_O + RO_IN * uz)
crotch_mid = arc_mid((xc, zc), R_CROTCH, crotch_on_A, crotch_on_B)

# ---------------- main strap profile (XZ), extruded along Y ----------------
prof = (
    cq.Workplane("XZ")
    .moveTo(-X_LO, Z_LEG_TOP)
    .lineTo(-X_LO, ZC_O)
    .threePointArc((0.0, 0.0), (X_LO, ZC_O))
    .lineTo(X_LO, Z_LEG_TOP)
    .lineTo(X_LI, Z_LEG_TOP)
    .lineTo(*bend_on_leg)
    .threePointArc(bend_mid, bend_on_arc)
    .threePointArc((0.0, ZC_I - RA_UP), mx(bend_on_arc))
    .threePointArc(mx(bend_mid), mx(bend_on_leg))
    .lineTo(-X_LI, Z_LEG_TOP)
    .close()
    # lens shaped opening between inner arc and outer band
    .moveTo(*crotch_on_A)
    .threePointArc((0.0, ZC_I - RA_LO), mx(crotch_on_A))
    .threePointArc(mx(crotch_mid), mx(crotch_on_B))
    .threePointArc((0.0, ZC_O - RO_IN), crotch_on_B)
    .threePointArc(crotch_mid, crotch_on_A)
    .close()
)
strap = prof.extrude(W / 2.0, both=True)
# round the long edges of the strap
strap = strap.faces(">Y or <Y").edges().fillet(EDGE_R)


# ---------------- hooks ----------------
def hook_profile():
    ro = 1.8           # outer corner radius of the lip
    ri = 0.4           # inner corner radius of the lip
    x_lo = HOOK_X
    x_li = x_lo - HOOK_T
    s = math.sqrt(0.5)
    w = (
        cq.Workplane("XZ")
        .moveTo(X_LO - 1.0, Z_TOP - HOOK_T)
        .lineTo(X_LO - 1.0, Z_TOP)
        .lineTo(x_lo - ro, Z_TOP)
        .threePointArc((x_lo - ro + ro * s, Z_TOP - ro + ro * s), (x_lo, Z_TOP - ro))
        .lineTo(x_lo, Z_TOP - HOOK_DROP)
        .lineTo(x_li, Z_TOP - HOOK_DROP)
        .lineTo(x_li, Z_TOP - HOOK_T - ri)
        .threePointArc((x_li - ri + ri * s, Z_TOP - HOOK_T - ri + ri * s), (x_li - ri, Z_TOP - HOOK_T))
        .close()
    )
    h = w.extrude(W_HOOK / 2.0, both=True)
    # rounded lip corners (seen from the side)
    h = h.edges("|X").edges("<Z").fillet(2.5)
    return h


# bend relief: the outside corners of the leg tops are bevelled down to the hook width
relief = (
    cq.Workplane("XY")
    .polyline([(X_LI - 0.01, W / 2.0 + 1.0), (X_LI - 0.01, W / 2.0), (X_LO, W_HOOK / 2.0),
               (X_LO + 1.0, W_HOOK / 2.0), (X_LO + 1.0, W / 2.0 + 1.0)])
    .close()
    .extrude(NOTCH_H + 1.0)
    .translate((0, 0, Z_TOP - NOTCH_H))
)
for r in (relief, relief.mirror("XZ")):
    strap = strap.cut(r).cut(r.mirror("YZ"))

hook_r = hook_profile()
hook_l = hook_r.mirror("YZ")
strap = strap.union(hook_r).union(hook_l)


# ---------------- oval holes ----------------
# leg holes (through X)
for z in LEG_HOLE_Z:
    c = (
        cq.Workplane("YZ")
        .center(0, z)
        .ellipse(LEG_HOLE_W / 2.0, LEG_HOLE_L / 2.0)
        .extrude(R_LEG + 10, both=True)
    )
    strap = strap.cut(c)

# inner arc holes (radial)
for k in range(ARC_HOLE_N):
    th = math.radians((k - (ARC_HOLE_N - 1) / 2.0) * ARC_HOLE_STEP)
    c = (
        cq.Workplane("XY")
        .ellipse(ARC_HOLE_L / 2.0, ARC_HOLE_W / 2.0)
        .extrude(2 * T, both=True)
    )
    c = c.rotate((0, 0, 0), (0, 1, 0), -math.degrees(th))
    c = c.translate((R_IN * math.sin(th), 0, ZC_I - R_IN * math.cos(th)))
    strap = strap.cut(c)

# shallow slits in the outside face of the outer band, along its -Y edge
ys = -W / 2.0 + SLIT_EDGE
for side in (-1, 1):
    for k in range(SLIT_N + 1):
        if side < 0 and k == 0:
            continue
        psi = k * SLIT_PITCH / R_LEG                   # angle from the bottom
        rs = RO_OUT - SLIT_DEPTH + 1.5
        s = (
            cq.Workplane("XY")
            .box(SLIT_LEN, SLIT_W, 3.0)
            .rotate((0, 0, 0), (0, 1, 0), -side * math.degrees(psi))
            .translate((side * rs * math.sin(psi), ys, ZC_O - rs * math.cos(psi)))
        )
        strap = strap.cut(s)

# ---------------- latch tabs with pegs ----------------
phi = math.radians(TAB_PHI)
px = RO_OUT * math.sin(phi)
pz = ZC_O - RO_OUT * math.cos(phi)
ang = phi - math.radians(TAB_FLARE)   # tab direction, measured from +X (right side)
tab = (
    cq.Workplane("XY")
    .box(TAB_L + 3.0, TAB_W, TAB_T, centered=(False, True, False))
    .edges("|Z and >X").fillet(2.0)
    .translate((-3.0, 0, -TAB_T))
    .rotate((0, 0, 0), (0, 1, 0), -math.degrees(ang))
    .translate((px, 0, pz))
)
# small cross peg (axis along Y) sitting on the outside of the tab at its -Y edge
t_out = (TAB_PEG_Z - (pz - TAB_T * math.cos(ang))) / math.sin(ang)
x_out = px + TAB_T * math.sin(ang) + t_out * math.cos(ang)   # tab outer face at the peg height
peg_x = x_out + PEG_D / 2.0 - PEG_EMBED
peg = (
    cq.Workplane("XZ")
    .center(peg_x, TAB_PEG_Z)
    .circle(PEG_D / 2.0)
    .extrude(-PEG_LEN)
    .translate((0, -W / 2.0, 0))
)
tab = tab.union(peg)
strap = strap.union(tab).union(tab.mirror("YZ"))

# cross pegs under the outer band (axis along Y, flush with the -Y edge)
for side in (-1, 1):
    th = math.asin(BOT_PEG_X / RO_OUT)
    rr = RO_OUT + PEG_D / 2.0 - BOT_PEG_EMBED
    bp = (
        cq.Workplane("XZ")
        .center(side * rr * math.sin(th), ZC_O - rr * math.cos(th))
        .circle(PEG_D / 2.0)
        .extrude(-PEG_LEN)
        .translate((0, -W / 2.0, 0))
    )
    strap = strap.union(bp)

result = strap

VIEW = {"azimuth": 45, "elevation": 26}
